import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------
# --- small spool / pulley (left body, centred on the origin) ---
SG_R_BODY = 18.2        # radius of slotted drum
SG_R_FLANGE = 19.2      # radius of bottom flange
SG_FLANGE_T = 2.0       # bottom flange height (where it meets the drum)
SG_BASE_H = 14.25       # total height of slotted drum incl. flange
SG_TOP_LIP = 0.9        # material above the pockets at the rim
SG_N_POCKETS = 12
SG_POCKET_W = 6.4       # pocket opening width at the skin
SG_POCKET_W_IN = 2.4    # width of pocket back face
SG_POCKET_DEPTH = 3.2   # radial pocket depth
SG_POCKET_TOP_DROP = 2.5   # pocket roof drops this much towards back face
SG_POCKET_BOT_RISE = 2.3   # pocket floor rises this much towards back face
SG_HUB_R = 11.2         # lower hub radius
SG_HUB_H = 6.7
SG_GROOVE_R = 8.6
SG_GROOVE_H = 3.75
SG_COLLAR_R = 11.2
SG_COLLAR_H = 4.9
SG_SQ = 11.0            # square drive boss side
SG_SQ_R = 2.0           # corner radius of square boss
SG_SQ_H = 3.0
SG_BORE = 3.8           # through bore
SG_TOP_ROUND = 1.2      # rounded top rim of the drum
SG_FLANGE_EDGE = 0.5    # vertical edge height of the bottom flange
SG_FLANGE_BULGE = 0.3   # outward bulge of the rounded flange bead
SG_CSK_D = 12.0         # countersink diameter at the underside

# --- large knob / disc (right body) ---
KD_X = 63.5             # centre distance between the two bodies
KD_R0 = 35.1            # circumradius of 32-gon wall
KD_N_SIDES = 32
KD_H = 12.5            # overall disc height (incl. top plateau)
KD_TAB_T = 0.9          # grip tab thickness
KD_TOP_N = 20           # top plateau polygon sides
KD_TOP_R = 33.9         # top plateau circumradius
KD_TOP_H = 0.4          # top plateau height
KD_HOLE = 4.0           # central blind hole in the top
KD_HOLE_DEPTH = 6.0
KD_REC_D = 55.5         # large shallow recess in underside
KD_REC_DEPTH = 1.0
KD_SEAT_D = 22.8        # circular seat for the spool collar
KD_SEAT_DEPTH = 1.0
KD_SOCK = 11.2          # square socket for the spool boss
KD_SOCK_R = 2.0
KD_SOCK_DEPTH = 3.5
KD_PIN_D = 3.9          # locating pin inside the socket
KD_PIN_GAP = 0.3        # pin end stands this far above the underside


# ---------------------------------------------------------------
# Small spool
# ---------------------------------------------------------------
def small_spool():
    # revolved envelope of the drum (flange + body)
    rr = SG_TOP_ROUND
    c45 = math.cos(math.radians(45))
    # convex rounded bead on the bottom flange
    ch_x = SG_R_BODY - SG_R_FLANGE
    ch_z = SG_FLANGE_T - SG_FLANGE_EDGE
    ch_l = math.hypot(ch_x, ch_z)
    fl_mid = (
        (SG_R_FLANGE + SG_R_BODY) / 2.0 + SG_FLANGE_BULGE * ch_z / ch_l,
        (SG_FLANGE_EDGE + SG_FLANGE_T) / 2.0 - SG_FLANGE_BULGE * ch_x / ch_l,
    )
    prof = (
        cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(SG_R_FLANGE, 0)
        .lineTo(SG_R_FLANGE, SG_FLANGE_EDGE)
        .threePointArc(fl_mid, (SG_R_BODY, SG_FLANGE_T))
        .lineTo(SG_R_BODY, SG_BASE_H - rr)
        .threePointArc(
            (SG_R_BODY - rr + rr * c45, SG_BASE_H - rr + rr * c45),
            (SG_R_BODY - rr, SG_BASE_H),
        )
        .lineTo(0, SG_BASE_H)
        .close()
    )
    body = prof.revolve(360, (0, 0, 0), (0, 1, 0))

    # 12 tapered (pyramid-frustum) pockets around the drum wall
    z_bot_out = SG_FLANGE_T
    z_top_out = SG_BASE_H - SG_TOP_LIP
    z_bot_in = z_bot_out + SG_POCKET_BOT_RISE
    z_top_in = z_top_out - SG_POCKET_TOP_DROP
    r_in = SG_R_BODY - SG_POCKET_DEPTH
    ext = 0.5  # carry the taper a little outside the skin
    kw = (SG_POCKET_W - SG_POCKET_W_IN) / 2.0 / SG_POCKET_DEPTH
    kt = (z_top_out - z_top_in) / SG_POCKET_DEPTH
    kb = (z_bot_in - z_bot_out) / SG_POCKET_DEPTH
    r_o = SG_R_BODY + ext
    hw_o = SG_POCKET_W / 2.0 + kw * ext
    zt_o = z_top_out + kt * ext
    zb_o = z_bot_out  # keep the floor clear of the flange bead
    hw_i = SG_POCKET_W_IN / 2.0

    def rect_wire(x, hw, zb, zt):
        return cq.Wire.makePolygon(
            [cq.Vector(x, -hw, zb), cq.Vector(x, hw, zb),
             cq.Vector(x, hw, zt), cq.Vector(x, -hw, zt)],
            close=True,
        )

    pocket = cq.Solid.makeLoft(
        [rect_wire(r_in, hw_i, z_bot_in, z_top_in), rect_wire(r_o, hw_o, zb_o, zt_o)],
        True,
    )
    pockets = None
    for i in range(SG_N_POCKETS):
        a = i * 360.0 / SG_N_POCKETS
        p = cq.Workplane("XY").add(pocket.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), a))
        pockets = p if pockets is None else pockets.union(p)
    body = body.cut(pockets)

    # stacked hub
    z = SG_BASE_H
    hub = cq.Workplane("XY").workplane(offset=z).circle(SG_HUB_R).extrude(SG_HUB_H)
    z += SG_HUB_H
    hub = hub.union(
        cq.Workplane("XY").workplane(offset=z).circle(SG_GROOVE_R).extrude(SG_GROOVE_H)
    )
    z += SG_GROOVE_H
    hub = hub.union(
        cq.Workplane("XY").workplane(offset=z).circle(SG_COLLAR_R).extrude(SG_COLLAR_H)
    )
    z += SG_COLLAR_H
    sq = (
        cq.Workplane("XY")
        .workplane(offset=z)
        .rect(SG_SQ, SG_SQ)
        .extrude(SG_SQ_H)
        .edges("|Z")
        .fillet(SG_SQ_R)
    )
    hub = hub.union(sq)
    z += SG_SQ_H
    total_h = z

    spool = body.union(hub)

    # through bore and underside countersink
    bore = cq.Workplane("XY").circle(SG_BORE / 2).extrude(total_h + 2).translate((0, 0, -1))
    csk_h = (SG_CSK_D - SG_BORE) / 2.0
    csk = cq.Solid.makeCone(SG_CSK_D / 2 + 0.5, SG_BORE / 2, csk_h + 0.5,
                            cq.Vector(0, 0, -0.5), cq.Vector(0, 0, 1))
    spool = spool.cut(bore).cut(cq.Workplane("XY").add(csk))
    return spool


# ---------------------------------------------------------------
# Large knob disc
# ---------------------------------------------------------------
def knob_disc():
    n = KD_N_SIDES
    pts = [
        (KD_R0 * math.cos(2 * math.pi * i / n), KD_R0 * math.sin(2 * math.pi * i / n))
        for i in range(n)
    ]
    h0 = KD_H - KD_TOP_H
    disc = cq.Workplane("XY").polyline(pts).close().extrude(h0)

    # grip tabs on every other facet
    side = 2 * KD_R0 * math.sin(math.pi / n)
    apothem = KD_R0 * math.cos(math.pi / n)
    step = 360.0 / n
    for k in range(n // 2):
        ang = step * 1.5 + k * 2 * step
        tab = (
            cq.Workplane("XY")
            .box(KD_TAB_T + 0.2, side, h0, centered=(False, True, False))
            .translate((apothem - 0.2, 0, 0))
            .rotate((0, 0, 0), (0, 0, 1), ang)
        )
        disc = disc.union(tab)

    # raised polygonal plateau on top
    tn = KD_TOP_N
    tpts = [
        (KD_TOP_R * math.cos(math.pi / 2 + 2 * math.pi * i / tn),
         KD_TOP_R * math.sin(math.pi / 2 + 2 * math.pi * i / tn))
        for i in range(tn)
    ]
    plateau = (
        cq.Workplane("XY").workplane(offset=h0 - 0.01)
        .polyline(tpts).close().extrude(KD_TOP_H + 0.01)
    )
    disc = disc.union(plateau)

    # central blind hole in the top
    blind = (
        cq.Workplane("XY").workplane(offset=KD_H - KD_HOLE_DEPTH)
        .circle(KD_HOLE / 2).extrude(KD_HOLE_DEPTH + 1)
    )
    disc = disc.cut(blind)

    # underside: shallow recess, collar seat, square socket
    rec = cq.Workplane("XY").circle(KD_REC_D / 2).extrude(KD_REC_DEPTH)
    seat = cq.Workplane("XY").circle(KD_SEAT_D / 2).extrude(KD_REC_DEPTH + KD_SEAT_DEPTH)
    sock = (
        cq.Workplane("XY")
        .rect(KD_SOCK, KD_SOCK)
        .extrude(KD_REC_DEPTH + KD_SEAT_DEPTH + KD_SOCK_DEPTH)
        .edges("|Z")
        .fillet(KD_SOCK_R)
    )
    disc = disc.cut(rec).cut(seat).cut(sock)
    # locating pin standing down from the socket floor
    z_floor = KD_REC_DEPTH + KD_SEAT_DEPTH + KD_SOCK_DEPTH
    pin = (
        cq.Workplane("XY").workplane(offset=KD_PIN_GAP)
        .circle(KD_PIN_D / 2).extrude(z_floor - KD_PIN_GAP + 0.01)
    )
    disc = disc.union(pin)
    return disc.translate((KD_X, 0, 0))


spool = small_spool()
knob = knob_disc()

result = spool.union(knob)

VIEW = {"azimuth": 45, "elevation": 26}
